import math
import cadquery as cq

# =====================================================================
#  Perforated sheet-metal basket / holder
#  - floor, back wall and two side walls with slanted front edges
#  - inward front flanges with rolled return posts and sloped caps
#  - large access window with inward return flange in the -X wall
#  - hexagonal perforation on floor, back wall and +X wall
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 186.0          # overall width  (X)
D = 190.0          # overall depth at the top (Y)
H = 98.5           # overall height (Z)
FLOOR_D = 143.7    # depth of the floor (outer, at the bottom)
T = 3.0            # sheet thickness
R_CORNER = 9.0     # outer radius of vertical back corners
R_FRONT = 11.0     # outer radius of front flange bends
R_FLOOR = 3.5      # outer radius of the floor bends
FLANGE_W = 19.7    # width of the inward front flanges (outer face -> free edge)
LIP_H = 3.5        # height of the lip along the floor front edge (along slant)
R_OPEN = 4.5       # corner radius of the front opening

# front corner posts (return plate + curl + sloped cap)
RET_YC = -55.0     # Y where the return's curl starts (= back end of the cap)
RET_RI = 12.0      # inner radius of the curl
RET_PHI = 60.0     # sweep angle of the curl (deg)
CAP_Z_BACK = 84.0  # height of cap top at the back end of the post
CAP_Z_FRONT = 97.0 # height of cap top near the front (at Y = YF_TOP + 2)

# -X side window
WIN_Y0 = 26.0      # window back edge, measured from back outer face
WIN_Y1 = 145.0     # window front edge, measured from back outer face
WIN_Z0 = 37.0      # window bottom (top of lower lip)
WIN_R = 0.5
WIN_RET = 3.5      # inward return flange around the window
WIN_RET_DROP = 2.5 # return flange stops this far below the top edge

YB = D / 2.0               # back outer face
YF_TOP = -D / 2.0          # top front
YF_BOT = YB - FLOOR_D      # bottom front

SL = math.hypot(YF_TOP - YF_BOT, H)                     # slant length
N_IN = cq.Vector(0, H / SL, -(YF_TOP - YF_BOT) / SL)    # inward normal of front
N_OUT = -N_IN
DYDZ = (YF_TOP - YF_BOT) / H                            # dY/dz along the front slant


def _sel(wp, pred):
    return [e for e in wp.edges().vals() if pred(e)]


def envelope(off, r_corner, r_front, top_extra=0.0):
    """Outer envelope of the basket shrunk inward by `off` (0 -> outer surface)."""
    yb = YB - off
    # front slant shifted inward along its normal
    y0 = YF_BOT + N_IN.y * off
    z0 = N_IN.z * off
    yf_bot = y0 + (off - z0) * DYDZ
    ztop = H + top_extra
    yf_top = y0 + (ztop - z0) * DYDZ
    hw = W / 2.0 - off
    env = (
        cq.Workplane("YZ")
        .polyline([(yf_bot, off), (yb, off), (yb, ztop), (yf_top, ztop)])
        .close()
        .extrude(hw, both=True)
    )

    def is_back_vertical(e):
        p0, p1 = e.startPoint(), e.endPoint()
        return (abs(p0.y - yb) < 1e-3 and abs(p1.y - yb) < 1e-3 and abs(p0.x - p1.x) < 1e-3
                and abs(abs(p0.x) - hw) < 1e-3)

    def is_front_slant(e):
        p0, p1 = e.startPoint(), e.endPoint()
        return (abs(p0.x - p1.x) < 1e-3 and abs(abs(p0.x) - hw) < 1e-3
                and abs(p0.z - p1.z) > 1 and abs(p0.y - p1.y) > 1)

    env = env.newObject(_sel(env, is_back_vertical)).fillet(r_corner)
    env = env.newObject(_sel(env, is_front_slant)).fillet(r_front)
    return env


# ---------------- main shell ----------------
outer = envelope(0.0, R_CORNER, R_FRONT)
outer = outer.faces("<Z").edges().fillet(R_FLOOR)
body = outer.faces(">Z").shell(-T)

# ---------------- front opening (leaves side flanges + floor lip) ----------------
front_plane = cq.Plane(origin=(0, YF_BOT, 0), xDir=(1, 0, 0), normal=N_OUT.toTuple())
ox = W / 2.0 - FLANGE_W
opening = (
    cq.Workplane(front_plane)
    .center(0, LIP_H + (SL + 20) / 2.0)
    .sketch()
    .rect(2 * ox, SL + 20)
    .vertices("<Y")
    .fillet(R_OPEN)
    .finalize()
    .extrude(T + 4, both=True)
)
body = body.cut(opening)

# ---------------- front corner posts ----------------
Y_CAP_B = RET_YC
slope = (CAP_Z_FRONT - CAP_Z_BACK) / (Y_CAP_B - (YF_TOP + 2.0))


def zcap(y):
    return CAP_Z_BACK + (Y_CAP_B - y) * slope


# mid-thickness envelope used to trim the posts so that their faces are buried
mid_env = envelope(T / 2.0, R_CORNER - T / 2.0, R_FRONT - T / 2.0, top_extra=5.0).val()


def post(side):
    xo = -ox  # center-facing face of the return (for the -X side)
    yfar = YF_TOP - 10
    c = (xo + RET_RI, RET_YC)          # centre of the curl (bends towards the box centre)
    phi = math.radians(RET_PHI)

    def on_arc(r, ang):
        return (c[0] - r * math.cos(ang), c[1] + r * math.sin(ang))

    ro = RET_RI + T
    ret = (
        cq.Workplane("XY")
        .moveTo(xo - T, yfar)
        .lineTo(xo - T, RET_YC)
        .threePointArc(on_arc(ro, phi / 2), on_arc(ro, phi))
        .lineTo(*on_arc(RET_RI, phi))
        .threePointArc(on_arc(RET_RI, phi / 2), (xo, RET_YC))
        .lineTo(xo, yfar)
        .close()
        .extrude(H + 5)
    )
    # sloped cap plate between side wall and return
    tz = T / math.cos(math.atan(slope))
    y0, y1 = yfar, Y_CAP_B
    x_in = -W / 2.0 + T / 2.0
    cap = (
        cq.Workplane("YZ", origin=(x_in, 0, 0))
        .polyline([(y0, zcap(y0)), (y1, zcap(y1)), (y1, zcap(y1) - tz), (y0, zcap(y0) - tz)])
        .close()
        .extrude(xo - x_in)
    )
    # below the cap top
    yb2 = Y_CAP_B + 20
    clip = (
        cq.Workplane("YZ", origin=(-W / 2.0 - 5, 0, 0))
        .polyline([(yfar, -5), (yb2, -5), (yb2, zcap(yb2)), (yfar, zcap(yfar))])
        .close()
        .extrude(W + 10)
    )
    p = ret.union(cap).intersect(clip).intersect(cq.Workplane().add(mid_env))
    if side > 0:
        p = p.mirror("YZ")
    return p


body = body.union(post(-1)).union(post(1))

# ---------------- -X side window with inward return flange ----------------
win_len = WIN_Y1 - WIN_Y0
win_h = H + 20 - WIN_Z0
wy = YB - (WIN_Y0 + WIN_Y1) / 2.0
wz = WIN_Z0 + win_h / 2.0


def win_sketch(grow, depth, x0):
    return (
        cq.Workplane("YZ", origin=(x0, 0, 0))
        .center(wy, wz)
        .sketch()
        .rect(win_len + 2 * grow, win_h + 2 * grow)
        .vertices("<Y")
        .fillet(WIN_R + grow)
        .finalize()
        .extrude(depth)
    )


collar = win_sketch(T, T / 2.0 + WIN_RET, -W / 2.0 + T / 2.0).cut(
    win_sketch(0, T + WIN_RET + 4, -W / 2.0 - 1)
)
collar = collar.intersect(cq.Workplane("XY").box(W, D, H - WIN_RET_DROP, centered=(True, True, False)))
body = body.cut(win_sketch(0, T + 4, -W / 2.0 - 2)).union(collar)

# ---------------- perforation: hexagonal holes + round holes ----------------
HEX_AF = 9.8                                    # hexagon across flats
HEX_D = HEX_AF / math.cos(math.radians(30))     # circumscribed diameter
P = 13.75                                       # hex pitch
PV = P * math.sqrt(3) / 2.0                     # row pitch
Z_MID_BACK = 50.3                               # middle hex row height, back wall
Z_MID_SIDE = 49.3                               # middle hex row height, side wall
RND_D = 6.4                                     # round hole diameter
CSK_D = 10.5                                    # countersink diameter (outer faces)


def hex_cutter(plane, pts, depth):
    return cq.Workplane(plane).pushPoints(pts).polygon(6, HEX_D).extrude(depth, both=True)


def csk_cutter(origin, direction, pts3d):
    """Through hole + 90 deg countersink starting at the outer face (origin plane)."""
    d = cq.Vector(*direction)
    h = (CSK_D - RND_D) / 2.0
    solids = []
    for p in pts3d:
        base = cq.Vector(*p)
        cyl = cq.Solid.makeCylinder(RND_D / 2.0, T + 4, base - d * 2.0, d)
        cone = cq.Solid.makeCone(CSK_D / 2.0 + 0.05, RND_D / 2.0, h + 0.05, base - d * 0.05, d)
        solids.append(cyl.fuse(cone))
    return cq.Workplane().add(cq.Compound.makeCompound(solids))


# back wall: local (x=Z, y=X); hexes pointing up
back_pl = cq.Plane(origin=(0, YB - T / 2.0, 0), xDir=(0, 0, 1), normal=(0, 1, 0))
back_pts = []
ZB = Z_MID_BACK
for k in range(-5, 6):
    back_pts.append((ZB, k * P))
for kk in (-4.5, -3.5, -1.5, -0.5, 0.5, 1.5, 3.5, 4.5):
    back_pts.append((ZB + PV, kk * P))
    back_pts.append((ZB - PV, kk * P))
for k in (-5, -4, 0, 4, 5):
    back_pts.append((ZB + 2 * PV, k * P))
    back_pts.append((ZB - 2 * PV, k * P))
back_rnd = [(x, YB, z) for x in (-31.5, 31.5) for z in (82.0, 19.2)]

# +X side wall: local (x=Z, y=-Y)
side_pl = cq.Plane(origin=(W / 2.0 - T / 2.0, 0, 0), xDir=(0, 0, 1), normal=(1, 0, 0))
side_pts = []
SIDE_A = 28.6     # first column of the odd rows, measured from the back outer face
SIDE_B = SIDE_A + P / 2.0
ZS = Z_MID_SIDE
for zrow, y0, n in (
    (ZS + 2 * PV, SIDE_A, 9),
    (ZS + PV, SIDE_B, 9),
    (ZS, SIDE_A, 9),
    (ZS - PV, SIDE_B, 8),
    (ZS - 2 * PV, SIDE_A, 8),
):
    for j in range(n):
        side_pts.append((zrow, -(YB - y0 - j * P)))

# floor: local (x=Y, y=-X); hexes pointing to front/back
floor_pl = cq.Plane(origin=(0, 0, T / 2.0), xDir=(0, 1, 0), normal=(0, 0, 1))
FLOOR_ROW0 = 24.8   # first hex row, measured from the back outer face
odd_all = list(range(0, 11))
even_all = list(range(0, 12))
floor_rows = [
    ("o", [0, 3, 4, 5, 6, 7, 8]),
    ("e", [0, 4, 5, 6, 7, 8, 9]),
    ("o", [0, 4, 5, 6, 7, 8]),
    ("e", even_all),
    ("o", odd_all),
    ("e", even_all),
    ("o", odd_all),
    ("e", even_all),
    ("o", [0, 3, 4, 5, 6, 7, 8]),
]
floor_pts = []
for i, (kind, ks) in enumerate(floor_rows):
    y = YB - (FLOOR_ROW0 + i * PV)
    for k in ks:
        x = (k - 5.5) * P if kind == "e" else (k - 5) * P
        floor_pts.append((y, -x))
floor_rnd = [(x, YB - y, 0.0) for x in (-44.4, 68.75) for y in (37.7, 133.5)]

cutters = (
    hex_cutter(back_pl, back_pts, T)
    .union(csk_cutter((0, YB, 0), (0, -1, 0), back_rnd))
    .union(hex_cutter(side_pl, side_pts, T))
    .union(hex_cutter(floor_pl, floor_pts, T))
    .union(csk_cutter((0, 0, 0), (0, 0, 1), floor_rnd))
)
body = body.cut(cutters)

result = body
